import cadquery as cq

# ---------------------------------------------------------------------------
# Welded steel junction box: open-top box with top flange and base plate,
# 45 deg gussets under the top flange, vertical ribs on the long faces,
# square flanged cable-entry bosses on every face, internal posts and trays.
# Units: mm.  X = length, Y = depth, Z = up.
# ---------------------------------------------------------------------------

FL_X = 580.0        # top flange / base plate length (X)
FL_Y = 500.0        # top flange / base plate width (Y)
H = 348.0           # overall height
T_TOP = 9.5         # top flange thickness
T_BOT = 10.0        # base plate thickness
OVH = 25.0          # flange overhang beyond the walls (= gusset leg, = rib depth)
T_WALL = 5.0        # wall thickness

WX = FL_X / 2 - OVH     # outer half length of walls
WY = FL_Y / 2 - OVH     # outer half width of walls
IX = WX - T_WALL        # inner half length
IY = WY - T_WALL        # inner half width

RIB_W = 24.0            # vertical rib width on the Y faces
RIB_XC = [-(WX - RIB_W / 2), 0.0, WX - RIB_W / 2]

# standard square entry boss
BOSS = 128.0
BOSS_T = 33.0
BORE = 80.0
BOLT_P = 99.0
BOLT_D = 14.0
BOSS_Z = 244.0          # centre height of upper bosses

# large entry boss (middle of -X face)
BIG = 188.0
BIG_BORE = 96.0
BIG_P = 154.0
BIG_Z = 229.0

# +X face: 2 rows x 3 bosses
ROW_Y = [-128.0, 0.0, 128.0]
LOW_Z = 73.0            # centre of lower row bolt pattern
LOW_TOP = LOW_Z + BOSS / 2

# front/back boss position along X
FB_X = 177.0
# -X face small bosses
LX_Y = BIG / 2 + BOSS / 2   # small bosses butt against the large one

# flange / base holes
FH_D = 14.0
FH_X = [-253.0, 0.0, 253.0]
FH_Y = 238.0

# internal posts
POST = 24.0
POST_H = 138.0
POST_HOLE = 12.0
POST_X = [-249.0, -11.5, 249.0]
POST_Y = 209.0

# internal trays
TRAY_X0 = -255.0
TRAY_X1 = 135.0
TRAY_W = 100.0
TRAY_H = 73.0
TRAY_T = 5.0
TRAY_Y = [-131.0, 0.0, 131.0]
TAB_L = 18.0
TAB_W = 46.0
SLOT_W = 30.0

# keep the weld seams between the individual plates/bosses as face splits
CLEAN = False


def U(a, b):
    return a.union(b, clean=CLEAN)


def C(a, b):
    return a.cut(b, clean=CLEAN)


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def wedge_x(w, y0, y1, zb, t):
    """45 deg drip wedge under a boss on the +X face (profile in XZ)."""
    return (cq.Workplane("XZ", origin=(0, y0, 0))
            .polyline([(w - 1.0, zb), (w + t, zb), (w - 1.0, zb - t - 1.0)])
            .close()
            .extrude(-(y1 - y0)))


def boss_px(w, yc, zc, size, t, z_lo=None, z_hi=None, wedge=True):
    """Square boss on a +X-facing wall whose outer face is at x = w."""
    z0 = zc - size / 2 if z_lo is None else z_lo
    z1 = zc + size / 2 if z_hi is None else z_hi
    y0, y1 = yc - size / 2, yc + size / 2
    b = box(w - 1.0, w + t, y0, y1, z0, z1)
    if wedge:
        b = U(b, wedge_x(w, y0, y1, z0, t))
    return b


def bore_px(w, yc, zc, d, t):
    return (cq.Workplane("YZ", origin=(w - T_WALL - 2.0, 0, 0))
            .center(yc, zc).circle(d / 2).extrude(t + T_WALL + 4.0))


def bolts_px(w, yc, zc, pitch, d, t):
    pts = [(yc + sy * pitch / 2, zc + sz * pitch / 2)
           for sy in (-1, 1) for sz in (-1, 1)]
    return (cq.Workplane("YZ", origin=(w + t + 1.0, 0, 0))
            .pushPoints(pts).circle(d / 2).extrude(-(t + 1.0)))


def rot(obj, ang):
    return obj.rotate((0, 0, 0), (0, 0, 1), ang)


# ---------------------------------------------------------------- main body
body = box(-WX, WX, -WY, WY, 0, H)
body = U(body, box(-FL_X / 2, FL_X / 2, -FL_Y / 2, FL_Y / 2, 0, T_BOT))
body = U(body, box(-FL_X / 2, FL_X / 2, -FL_Y / 2, FL_Y / 2, H - T_TOP, H))

# 45 deg gussets under the top flange: the X-side gussets run the full
# flange width (flat ends flush with the flange), the Y-side ones between walls
ZG = H - T_TOP
gx = (cq.Workplane("XZ", origin=(0, FL_Y / 2, 0))
      .polyline([(WX - 1.0, ZG), (FL_X / 2, ZG), (WX - 1.0, ZG - OVH - 1.0)])
      .close().extrude(FL_Y))
gy = (cq.Workplane("YZ", origin=(-WX, 0, 0))
      .polyline([(WY - 1.0, ZG), (FL_Y / 2, ZG), (WY - 1.0, ZG - OVH - 1.0)])
      .close().extrude(2 * WX))
for g in (gx, gx.mirror("YZ"), gy, gy.mirror("XZ")):
    body = U(body, g)

# vertical ribs on the front and back faces
for sy in (-1, 1):
    for xc in RIB_XC:
        y0, y1 = (WY - 1.0, FL_Y / 2) if sy > 0 else (-FL_Y / 2, -WY + 1.0)
        body = U(body, box(xc - RIB_W / 2, xc + RIB_W / 2, y0, y1,
                           T_BOT - 1.0, H - T_TOP + 1.0))

# --------------------------------------------------------------- cavity
body = C(body, box(-IX, IX, -IY, IY, T_BOT, H + 1.0))

# ------------------------------------------------------------- internal posts
for px in POST_X:
    for sy in (-1, 1):
        py = sy * POST_Y
        post = box(px - POST / 2, px + POST / 2, py - POST / 2, py + POST / 2,
                   T_BOT - 1.0, POST_H)
        hole = (cq.Workplane("XY", origin=(0, 0, POST_H - 30.0))
                .center(px, py).circle(POST_HOLE / 2).extrude(31.0))
        body = U(body, C(post, hole))

# ------------------------------------------------------------- internal trays
for ty in TRAY_Y:
    y0, y1 = ty - TRAY_W / 2, ty + TRAY_W / 2
    tray = box(TRAY_X0, TRAY_X1, y0, y1, T_BOT - 1.0, TRAY_H)
    tray = C(tray, box(TRAY_X0 + TRAY_T, TRAY_X1 - TRAY_T,
                       y0 + TRAY_T, y1 - TRAY_T, T_BOT + 4.0, TRAY_H + 1.0))
    # clip tabs at both ends
    for sx in (-1, 1):
        xw = TRAY_X1 - TRAY_T if sx > 0 else TRAY_X0 + TRAY_T   # inner end face
        xa, xb = sorted((xw + sx * 1.0, xw - sx * TAB_L))
        tab = box(xa, xb, ty - TAB_W / 2, ty + TAB_W / 2, T_BOT + 3.0, TRAY_H)
        sa, sb = sorted((xw, xw - sx * (TAB_L - 3.0)))
        slot = box(sa, sb, ty - SLOT_W / 2, ty + SLOT_W / 2,
                   T_BOT + 8.0, TRAY_H + 1.0)
        tray = U(tray, C(tab, slot))
    body = U(body, tray)

# ------------------------------------------------------------ entry bosses
bosses = []
cut_list = []


def add_boss(ang, w, yc, zc, size, bore, pitch, **kw):
    bosses.append(rot(boss_px(w, yc, zc, size, BOSS_T, **kw), ang))
    cut_list.append(rot(bore_px(w, yc, zc, bore, BOSS_T), ang))
    cut_list.append(rot(bolts_px(w, yc, zc, pitch, BOLT_D, BOSS_T), ang))


# +X face: upper row (with drip wedge) and lower row (down to base bottom)
for yc in ROW_Y:
    add_boss(0, WX, yc, BOSS_Z, BOSS, BORE, BOLT_P)
    add_boss(0, WX, yc, LOW_Z, BOSS, BORE, BOLT_P,
             z_lo=0.0, z_hi=LOW_TOP, wedge=False)

# -Y (front) face boss: rotate -90 (local y -> global X)
add_boss(-90, WY, FB_X, BOSS_Z, BOSS, BORE, BOLT_P)
# +Y (back) face boss: rotate +90 (local y -> global -X)
add_boss(90, WY, -FB_X, BOSS_Z, BOSS, BORE, BOLT_P)
# -X face: small, large, small (rotate 180: local y -> global -Y)
add_boss(180, WX, -LX_Y, BOSS_Z, BOSS, BORE, BOLT_P)
add_boss(180, WX, LX_Y, BOSS_Z, BOSS, BORE, BOLT_P)
add_boss(180, WX, 0.0, BIG_Z, BIG, BIG_BORE, BIG_P)

for b in bosses:
    body = U(body, b)
for c in cut_list:
    body = C(body, c)

# ------------------------------------------------ flange and base-plate holes
pts = [(x, sy * FH_Y) for x in FH_X for sy in (-1, 1)]
top_holes = (cq.Workplane("XY", origin=(0, 0, H - 30.0))
             .pushPoints(pts).circle(FH_D / 2).extrude(31.0))
bot_holes = (cq.Workplane("XY", origin=(0, 0, -1.0))
             .pushPoints(pts).circle(FH_D / 2).extrude(T_BOT + 1.0))
body = C(C(body, top_holes), bot_holes)

# -------------------------------------------------------------- tidy faces
# Merge coplanar face fragments left by the boolean steps, but keep the seam
# edges between individually welded pieces (entry bosses side by side, boss /
# drip wedge joints, rib / flange / gusset joints on the long faces).
TOL = 1e-3
DIVIDERS = [(ROW_Y[i] + ROW_Y[i + 1]) / 2 for i in range(len(ROW_Y) - 1)]
WEDGE_Z = [BOSS_Z - BOSS / 2, BIG_Z - BIG / 2]


def keep_edge(e):
    if e.geomType() != "LINE":
        return False
    a, b = e.startPoint(), e.endPoint()
    # seams on the flush front/back planes (flange, ribs, gussets, base)
    if abs(abs(a.y) - FL_Y / 2) < TOL and abs(a.y - b.y) < TOL:
        return True
    # seams between neighbouring bosses on the +X face (not on the base)
    for yd in DIVIDERS:
        if (abs(a.y - yd) < TOL and abs(b.y - yd) < TOL
                and min(a.x, b.x) > WX - TOL and max(a.z, b.z) > 0.5):
            return True
    # boss / drip wedge joints on the boss side faces
    for zw in WEDGE_Z:
        if (abs(a.z - zw) < TOL and abs(b.z - zw) < TOL
                and abs(e.Length() - BOSS_T) < 1.5):
            return True
    return False


try:
    from OCP.ShapeUpgrade import ShapeUpgrade_UnifySameDomain
    shp = body.val()
    usd = ShapeUpgrade_UnifySameDomain(shp.wrapped, True, True, True)
    for ed in shp.Edges():
        if keep_edge(ed):
            usd.KeepShape(ed.wrapped)
    usd.Build()
    tidy = cq.Shape.cast(usd.Shape())
    sols = tidy.Solids()
    if len(sols) == 1 and sols[0].isValid():
        body = cq.Workplane("XY").newObject([sols[0]])
    elif tidy.isValid():
        body = cq.Workplane("XY").newObject([tidy])
except Exception:
    body = body.clean()

result = body

VIEW = {"azimuth": 45, "elevation": 26}
